import math
import cadquery as cq

# =====================================================================
# Depth-camera style body on a small swivel stand.
# Local frame: body long axis = Y, lens face = +X, Z up, base bottom z=0.
# The finished part is yawed about Z by YAW.
# =====================================================================

YAW = 26.0             # whole part rotated about Z (deg)

# ---------------- camera body (stadium prism) ----------------
BODY_L = 100.0         # overall length (tip to tip)
BODY_W = 23.6          # depth (front face to back face)
BODY_H = 18.15
BODY_EDGE_R = 0.5

# recessed stadium lens panel on the front (+X) face
PANEL_L = 75.5
PANEL_H = 9.2
PANEL_DEPTH = 0.8
PANEL_DZ = 1.0         # panel centre above body mid-height

LENS_Y = [-27.0, 8.6, 24.7]
LENS_RING_D = 8.4
LENS_RING_DEPTH = 0.8
LENS_DOME_D = 6.4
LENS_DOME_H = 2.4

HOLE_D = 1.5
HOLE_DEPTH = 0.8
# (y, dz) of the small sensor holes, dz relative to panel centre
HOLES = [(-9.8, 1.8), (-9.8, -2.8), (16.9, 0.3), (32.6, 0.3)]

# ---------------- neck (swivel block) ----------------
NECK_CX = 0.7          # centre, local X (across body)
NECK_CY = 1.4          # centre, local Y (along body)
NECK_X = 25.1          # size across the body
NECK_Y = 19.8          # size along the body
NECK_H = 7.6
NECK_TOP_R = 4.5       # top round along the two long sides
NECK_END_R = 5.0       # top round along the two short ends
NECK_CORNER_R = 3.5    # two diagonally opposite vertical corners
NECK_YAW = 5.0         # extra swivel of the neck relative to body

# ---------------- base plate ----------------
BASE_CX = 1.7
BASE_CY = -1.55
BASE_X = 41.9
BASE_Y = 31.2
BASE_H = 7.1
BASE_SIDE_R = 3.0      # top round along the two long sides
BASE_BOT_R = 1.5       # bottom round along the two long sides
BASE_NOSE_R = 3.45     # bull-nose at the front (+X) end
BASE_BACK_R = 2.0      # round on the back (-X) end
TRIPOD_D = 8.8
TRIPOD_DEPTH = 9.0
TRIPOD_X = -1.8
TRIPOD_Y = 2.35

BIG = 200.0


def lens_dome(a, h):
    """Spherical cap: base radius a, height h, axis +X, base at x=0."""
    R = (a * a + h * h) / (2 * h)
    cx = h - R
    phi0 = math.asin(a / R) if a < R else math.pi / 2
    pm = phi0 / 2
    prof = (
        cq.Workplane("XY")
        .moveTo(0, 0)
        .lineTo(0, a)
        .threePointArc((cx + R * math.cos(pm), R * math.sin(pm)), (h, 0))
        .close()
    )
    return prof.revolve(360, (0, 0, 0), (1, 0, 0))


def rounded_profile(w, h, r_tl, r_tr, r_br=0.0, r_bl=0.0):
    """Closed 2D profile (x in [-w/2, w/2], y in [0, h]) with optional
    rounded corners (tl = top-left, tr = top-right, ...)."""
    x0, x1 = -w / 2, w / 2
    k = 1 - math.sqrt(0.5)
    wp = cq.Workplane("XY").moveTo(x0 + r_bl, 0)
    wp = wp.lineTo(x1 - r_br, 0)
    if r_br > 0:
        wp = wp.threePointArc((x1 - r_br * k, r_br * k), (x1, r_br))
    wp = wp.lineTo(x1, h - r_tr)
    if r_tr > 0:
        wp = wp.threePointArc((x1 - r_tr * k, h - r_tr * k), (x1 - r_tr, h))
    wp = wp.lineTo(x0 + r_tl, h)
    if r_tl > 0:
        wp = wp.threePointArc((x0 + r_tl * k, h - r_tl * k), (x0, h - r_tl))
    wp = wp.lineTo(x0, r_bl)
    if r_bl > 0:
        wp = wp.threePointArc((x0 + r_bl * k, r_bl * k), (x0 + r_bl, 0))
    return wp.close()


def profile_solid(plane, w, h, length, **radii):
    """Extrude a rounded_profile drawn on 'XZ' (runs along Y) or 'YZ'
    (runs along X) symmetrically by length."""
    prof = rounded_profile(w, h, **radii)
    solid = prof.extrude(length / 2, both=True).val()
    if plane == "XZ":      # profile in local X-Z, extruded along Y
        solid = solid.rotate((0, 0, 0), (1, 0, 0), 90)
    else:                  # profile in local Y-Z, extruded along X
        solid = solid.rotate((0, 0, 0), (1, 0, 0), 90)
        solid = solid.rotate((0, 0, 0), (0, 0, 1), 90)
    return cq.Workplane("XY").add(solid)


# ---------------- base plate ----------------
# side profile (rounded top edges along the long sides), run across the
# body; then the front end is rounded into a bull-nose and the back end
# gets a smaller round on its top/vertical edges.
base_prof = rounded_profile(
    BASE_Y, BASE_H, r_tl=BASE_SIDE_R, r_tr=BASE_SIDE_R,
    r_bl=BASE_BOT_R, r_br=BASE_BOT_R,
)
base = cq.Workplane("XY").add(
    base_prof.extrude(BASE_X / 2, both=True)
    .val()
    .rotate((0, 0, 0), (1, 0, 0), 90)
    .rotate((0, 0, 0), (0, 0, 1), 90)
)
base = base.faces(">X").edges().fillet(BASE_NOSE_R)
base = base.faces("<X").edges().fillet(BASE_BACK_R)
base = base.translate((BASE_CX, BASE_CY, 0))

# ---------------- neck ----------------
nx, ny, rc = NECK_X / 2, NECK_Y / 2, NECK_CORNER_R
k = 1 - math.sqrt(0.5)
neck_plan = (
    cq.Workplane("XY")
    .moveTo(-nx + rc, -ny)
    .lineTo(nx, -ny)
    .lineTo(nx, ny - rc)
    .threePointArc((nx - rc * k, ny - rc * k), (nx - rc, ny))
    .lineTo(-nx, ny)
    .lineTo(-nx, -ny + rc)
    .threePointArc((-nx + rc * k, -ny + rc * k), (-nx + rc, -ny))
    .close()
    .extrude(NECK_H + 0.2)
)
neck_side = profile_solid(
    "XZ", NECK_X, NECK_H + 0.2, BIG, r_tl=NECK_TOP_R, r_tr=NECK_TOP_R
)
neck_end = profile_solid(
    "YZ", NECK_Y, NECK_H + 0.2, BIG, r_tl=NECK_END_R, r_tr=NECK_END_R
)
neck = neck_plan.intersect(neck_side).intersect(neck_end)
neck = neck.rotate((0, 0, 0), (0, 0, 1), NECK_YAW).translate(
    (NECK_CX, NECK_CY, BASE_H - 0.1)
)

# ---------------- body ----------------
z0 = BASE_H + NECK_H
body = (
    cq.Workplane("XY")
    .workplane(offset=z0)
    .slot2D(BODY_L, BODY_W, angle=90)
    .extrude(BODY_H)
    .edges("not |Z")
    .fillet(BODY_EDGE_R)
)

zc = z0 + BODY_H / 2 + PANEL_DZ
face_x = BODY_W / 2
floor_x = face_x - PANEL_DEPTH

panel = (
    cq.Workplane("YZ", origin=(floor_x, 0, zc))
    .slot2D(PANEL_L, PANEL_H, angle=0)
    .extrude(5.0)
)
body = body.cut(panel)

for y in LENS_Y:
    ring = (
        cq.Workplane("YZ", origin=(floor_x - LENS_RING_DEPTH, y, zc))
        .circle(LENS_RING_D / 2)
        .extrude(LENS_RING_DEPTH + 0.1)
    )
    body = body.cut(ring)
    dome = lens_dome(LENS_DOME_D / 2, LENS_DOME_H).translate(
        (floor_x - LENS_RING_DEPTH - 0.02, y, zc)
    )
    body = body.union(dome)

for (y, dz) in HOLES:
    h = (
        cq.Workplane("YZ", origin=(floor_x - HOLE_DEPTH, y, zc + dz))
        .circle(HOLE_D / 2)
        .extrude(HOLE_DEPTH + 0.1)
    )
    body = body.cut(h)

part = base.union(neck).union(body)
# tripod screw hole in the underside
part = part.cut(
    cq.Workplane("XY").center(TRIPOD_X, TRIPOD_Y).circle(TRIPOD_D / 2).extrude(TRIPOD_DEPTH)
)
result = part.rotate((0, 0, 0), (0, 0, 1), YAW)
